import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
S = 0.4                      # reference-pixel -> mm scale used while measuring

R_OUT = 92.0 * S             # outer radius of housing / front disc
R_WALL_IN = 82.0 * S         # inner radius of housing wall
DEPTH = 70.0 * S             # overall depth (front face y=0 -> back y=DEPTH)
T_PLATE = 13.8 * S           # grille plate thickness
T_LUG = 18.0 * S             # mounting lug thickness

LUG_ANGLES = [95.2, 165.0, -15.0, 275.2]   # deg, in the front (XZ) plane
LUG_HOLE_R = 105.2 * S       # radius of lug hole centres
LUG_END_R = 13.8 * S         # radius of rounded lug ends
LUG_HOLE_D = 15.0 * S
LUG_TAPER = 21.6             # deg, side taper of lugs

R_BORE = 50.0 * S            # air bore radius behind the grille
FAN_Y0 = 35.0 * S            # fan mounting flange (inside housing)
FAN_Y1 = 49.0 * S
FAN_HOLE_R = 63.3 * S
FAN_HOLE_D = 12.7 * S
FAN_HOLE_ANGLES = [0, 180]

# blocks in front of the flange (top and bottom), carrying vertical screw holes
TB_Y0 = 20.8 * S             # top block front face
TB_A0, TB_A1 = 67.5, 118.0   # top block angular extent (deg)
BB_Y0 = T_PLATE              # bottom block front face
BB_A0, BB_A1 = -112.0, -68.0
VH_X = 0.0
VH_Y = 34.5 * S
VH_D = 12.7 * S
BLK_FILLET = 3.5 * S         # convex front edge of the top block side face
FOOT_FILLET = 3.0 * S        # concave foot of the top block side face

# side opening (rotated frame u along SLOT_ANG)
SLOT_ANG = 40.0
SLOT_U0 = 27.5 * S
SLOT_V_LO = -43.0 * S
SLOT_V_HI = 39.0 * S
RING_KEEP_R = 57.0 * S       # flange ring left standing in the opening
EAR_R = 78.5 * S
EAR_HI_P = (34.2 * S, 52.85 * S)   # point on upper ear side
EAR_HI_DIR = 57.0                  # direction of upper ear side (deg)
EAR_LO_P = (60.0 * S, 16.3 * S)    # point on lower ear top
EAR_LO_DIR = 0.0
EAR_FILLET = 6.0 * S
EAR_LO_FILLET = 8.0 * S

# cross screw hole through top & bottom of housing
XHOLE_Y = 57.0 * S
XHOLE_D = 15.0 * S
BOSS_Z = 74.8 * S            # inner flats for the cross screw
BOSS_Y0 = FAN_Y1

# grille slots: (x centre, z top, z bottom) in reference px (scaled by S)
SLOT_W = 6.8 * S
GRILLE = [
    (-63.4, 28.0, -33.7),
    (-48.0, 46.9, -48.7),
    (-32.8, 60.7, -63.2),
    (-17.1, 62.6, -67.9),
    (-1.5, 29.5, -67.1),
    (13.9, 11.8, -56.8),
    (29.7, -4.4, -45.2),
    (45.0, -18.6, -39.4),
]


# ---------------- helpers ----------------
def xz(y_back):
    """XZ workplane located at y_back (local x = X, local y = Z, normal -Y)."""
    return cq.Workplane("XZ", origin=(0, y_back, 0))


def disc(r, y0, y1):
    return xz(y1).circle(r).extrude(y1 - y0)


def ring(r0, r1, y0, y1):
    return xz(y1).circle(r1).circle(r0).extrude(y1 - y0)


def polar(r, a_deg):
    a = math.radians(a_deg)
    return (r * math.cos(a), r * math.sin(a))


def sector(r0, r1, a0, a1, y0, y1):
    am = 0.5 * (a0 + a1)
    w = (xz(y1).moveTo(*polar(r0, a0)).lineTo(*polar(r1, a0))
         .threePointArc(polar(r1, am), polar(r1, a1))
         .lineTo(*polar(r0, a1))
         .threePointArc(polar(r0, am), polar(r0, a0))
         .close())
    return w.extrude(y1 - y0)


def halfplane(p, dir_deg, y0, y1, size=400.0):
    """prism of the half plane lying to the left of the directed line through p."""
    d = (math.cos(math.radians(dir_deg)), math.sin(math.radians(dir_deg)))
    n = (-d[1], d[0])
    a = (p[0] - size * d[0], p[1] - size * d[1])
    b = (p[0] + size * d[0], p[1] + size * d[1])
    c = (b[0] + size * n[0], b[1] + size * n[1])
    e = (a[0] + size * n[0], a[1] + size * n[1])
    return xz(y1).polyline([a, b, c, e]).close().extrude(y1 - y0)


def line_circle(p, dir_deg, r):
    """intersection of line (p, dir) with circle r (point nearest to p)."""
    d = (math.cos(math.radians(dir_deg)), math.sin(math.radians(dir_deg)))
    b = p[0] * d[0] + p[1] * d[1]
    c = p[0] ** 2 + p[1] ** 2 - r * r
    disc_ = math.sqrt(max(b * b - c, 0.0))
    ts = [-b + disc_, -b - disc_]
    t = min(ts, key=abs)
    return (p[0] + t * d[0], p[1] + t * d[1])


def edge_box(pt, y0, y1, tol=0.6):
    """selector for edges whose centre lies near XZ point pt within y range."""
    return cq.selectors.BoxSelector((pt[0] - tol, y0, pt[1] - tol),
                                    (pt[0] + tol, y1, pt[1] + tol))


def lug(ang):
    a = math.radians(ang)
    d = (math.cos(a), math.sin(a))
    n = (-math.sin(a), math.cos(a))
    t = math.radians(LUG_TAPER)

    def g(ax, lat):
        return (ax * d[0] + lat * n[0], ax * d[1] + lat * n[1])

    base_ax = R_OUT * 0.72
    side = []
    for s in (1, -1):
        tx = LUG_HOLE_R + LUG_END_R * math.sin(t)
        ty = s * LUG_END_R * math.cos(t)
        by = ty + s * (tx - base_ax) * math.tan(t)
        side.append(((tx, ty), (base_ax, by)))
    (t1, b1), (t2, b2) = side
    return (xz(T_LUG).moveTo(*g(*b2)).lineTo(*g(*t2))
            .threePointArc(g(LUG_HOLE_R + LUG_END_R, 0.0), g(*t1))
            .lineTo(*g(*b1)).close().extrude(T_LUG))


# ---------------- main body ----------------
body = disc(R_OUT, 0, DEPTH)
for a in LUG_ANGLES:
    body = body.union(lug(a))

# hollow housing behind the grille plate
body = body.cut(disc(R_WALL_IN, T_PLATE, DEPTH))

# fan mounting flange + blocks in front of it
body = body.union(ring(R_BORE, R_WALL_IN + 0.3, FAN_Y0, FAN_Y1))
body = body.union(sector(R_BORE, R_WALL_IN + 0.3, TB_A0, TB_A1, TB_Y0, FAN_Y0))
body = body.union(sector(R_BORE, R_WALL_IN + 0.3, BB_A0, BB_A1, BB_Y0 - 0.2, FAN_Y0))

# inner flats (bosses) for the cross screw, top & bottom
for sgn in (1, -1):
    boss = (xz(DEPTH).center(0, sgn * (BOSS_Z + 20))
            .rect(2 * R_OUT, 40).extrude(DEPTH - BOSS_Y0))
    boss = boss.intersect(disc(R_WALL_IN + 0.3, BOSS_Y0, DEPTH))
    body = body.union(boss)

# lug holes
for a in LUG_ANGLES:
    body = body.cut(xz(T_LUG + 1).center(*polar(LUG_HOLE_R, a))
                    .circle(LUG_HOLE_D / 2).extrude(T_LUG + 2))

# fan holes in the flange
for a in FAN_HOLE_ANGLES:
    body = body.cut(xz(FAN_Y1 + 1).center(*polar(FAN_HOLE_R, a))
                    .circle(FAN_HOLE_D / 2).extrude(FAN_Y1 - FAN_Y0 + 2))

# grille slots
for (x, zt, zb) in GRILLE:
    x, zt, zb = x * S, zt * S, zb * S
    body = body.cut(xz(T_PLATE + 1).center(x, (zt + zb) / 2)
                    .slot2D(zt - zb, SLOT_W, angle=90).extrude(T_PLATE + 2))

# ---------------- side opening ----------------
big = 4 * R_OUT
opening = (xz(DEPTH + 1)
           .transformed(rotate=(0, 0, SLOT_ANG))
           .center(SLOT_U0 + big / 2, (SLOT_V_LO + SLOT_V_HI) / 2)
           .rect(big, SLOT_V_HI - SLOT_V_LO)
           .extrude(DEPTH + 2))
# material left standing inside the opening
keep = disc(RING_KEEP_R, FAN_Y0, FAN_Y1)
ear_hi = halfplane(EAR_HI_P, EAR_HI_DIR, FAN_Y0, FAN_Y1).intersect(disc(EAR_R, FAN_Y0, FAN_Y1))
ear_lo = halfplane(EAR_LO_P, EAR_LO_DIR + 180.0, FAN_Y0, FAN_Y1).intersect(disc(EAR_R, FAN_Y0, FAN_Y1))
blk_keep = sector(0.1, EAR_R, TB_A0, TB_A1, TB_Y0, FAN_Y0)
keep = keep.union(ear_hi).union(ear_lo)


# concave fillets where the ears meet the ring
for p, dd, rr in ((EAR_HI_P, EAR_HI_DIR, EAR_FILLET), (EAR_LO_P, EAR_LO_DIR, EAR_LO_FILLET)):
    c = line_circle(p, dd, RING_KEEP_R)
    keep = keep.edges(edge_box(c, FAN_Y0 - 1, FAN_Y1 + 1)).fillet(rr)
keep = keep.union(blk_keep)
opening = opening.cut(keep)
body = body.cut(opening)

# vertical screw holes through the blocks
body = body.cut(cq.Workplane("XY", origin=(VH_X, VH_Y, -R_WALL_IN))
                .circle(VH_D / 2).extrude(2 * R_WALL_IN))

# cross screw holes (vertical) through the top and bottom wall + inner flats
for sgn in (1, -1):
    z0 = sgn * (BOSS_Z - 0.5)
    body = body.cut(cq.Workplane("XY", origin=(0, XHOLE_Y, z0))
                    .circle(XHOLE_D / 2).extrude(sgn * (R_OUT - BOSS_Z + 3)))

# soften the step between the top block and the flange (visible in the opening)
body = body.clean()
p_mid = polar(0.5 * (R_BORE + EAR_R), TB_A0)
body = body.edges(edge_box(p_mid, TB_Y0 - 0.3, TB_Y0 + 0.3, tol=1.0)).fillet(BLK_FILLET)

# concave fillet at the foot of the block side face
a = math.radians(TB_A0)
d_rad = cq.Vector(math.cos(a), 0, math.sin(a))
t_dir = cq.Vector(math.sin(a), 0, -math.cos(a))
rf = FOOT_FILLET
k = rf * (1 - math.sqrt(0.5))
foot = (cq.Workplane(cq.Plane(origin=d_rad * (R_BORE - 1.0), xDir=t_dir, normal=d_rad))
        .moveTo(0, FAN_Y0 + 0.05).lineTo(0, FAN_Y0 - rf)
        .threePointArc((k, FAN_Y0 - k), (rf, FAN_Y0))
        .lineTo(rf, FAN_Y0 + 0.05).close()
        .extrude(EAR_R - R_BORE + 2.0))
foot = foot.intersect(ring(R_BORE, EAR_R, TB_Y0, FAN_Y1))
body = body.union(foot).clean()

result = body.clean()
